import math
import cadquery as cq

# ---------------------------------------------------------------
# Driving dimensions (mm)
# X = plate width, Y = plate length (hinge at -Y, shaft bracket at +Y)
# ---------------------------------------------------------------
W = 126.4          # main plate width (X)
L = 187.7          # main plate length (Y)
T_MAIN = 11.8      # main plate thickness
T_LOW = 6.8        # thickness of the recessed strip at the hinge end
CORNER_R = 3.0     # plate corner rounding at the -Y corners
CORNER_C = 3.6     # chamfer at the -X/+Y plate corner

# hinge (knuckles)
HY = 52.2          # hinge axis Y
HZ = 12.1          # hinge axis Z
KR = 6.2           # knuckle outer radius
PIN_R = 2.7        # pin hole radius
K_W = 6.8          # knuckle width
K_PITCH = 15.1     # knuckle pitch
K_START = 13.9     # X start of 2nd knuckle (1st one is clipped by the edge)
N_K = 9
FOOT_R = 3.8       # concave S-curve radius at the knuckle foot
NOTCH_Y = 58.9     # back wall of the clearance notches between knuckles
NOTCH_R = 3.4      # rounded top edge of the notch back wall
NOTCH_Z = T_LOW

# bosses / holes at the hinge end
HOLE_X = 7.6
HOLE_Y1 = 7.9
HOLE_Y2 = 37.7
BOSS_TOP = 10.2
CBOSS_R = 6.8      # corner boss radius
BOSS_R = 5.8       # second row boss radius
HOLE_R = 3.2

# centre counterbore
CH_X = W / 2
CH_Y = 118.3
CB_R = 13.7
CB_D = 5.3
CH_R = 4.5

# blind holes from below around the centre hole
BH_OFF = 49.0
BH_R = 4.4
BH_D = 8.0

# bracket at +Y end
T_BASE = 8.0
BAR_Y = 198.5                 # +Y edge of the bar joining the saddles
S_W = 13.4                    # saddle block width (X)
S_OFF = 36.8                  # saddle centre offset from plate centre
S_Y0, S_Y1 = 183.0, 236.5     # saddle block Y extent
S_TOP = 18.8
S_FR = 1.5                    # saddle vertical edge rounding
U_Y = 209.0                   # shaft axis Y
U_Z = 20.0                    # shaft axis Z
U_R = 13.7                    # shaft seat radius
LIP_R = 12.2                  # lip (shoulder) radius
LIP_W = 4.8                   # lip width (outer side)
S_HOLE_R = 3.5
S_HOLE_Y = (189.0, 229.5)     # saddle screw hole positions (Y)
S_HOLE_D = 12.0

TAB_Y0, TAB_Y1 = 192.7, 209.0
TAB_X1 = 157.7
TAB_BLK_L = 11.9
TAB_BLK_TOP = 19.4
TAB_BLK_R = 1.8
TAB_FIL = 10.0
DIAG_SLOPE = 0.41             # dX/dY of the +X side diagonal edge
TAB_FIL2 = 4.5


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


# ---------------------------------------------------------------
# main plate: low level everywhere, raised slab behind the hinge
# ---------------------------------------------------------------
plate = box(0, W, 0, L, 0, T_LOW)
plate = plate.union(box(0, W, HY, L, 0, T_MAIN))
plate = plate.clean()
for _p in ((0, 0, 1), (W, 0, 1)):
    plate = (plate.edges("|Z")
             .edges(cq.selectors.NearestToPointSelector(_p))
             .fillet(CORNER_R))
plate = (plate.edges("|Z")
         .edges(cq.selectors.NearestToPointSelector((0, L, 5)))
         .chamfer(CORNER_C))

# knuckle profile (YZ): S-shaped foot on the -Y side (concave curve tangent
# to the low floor, blending into the knuckle circle), round top, merging
# into the raised slab on the +Y side.  The outer contour is one smooth
# spline through points of the underlying arc construction.
_h = HZ - T_LOW - FOOT_R
_dy = math.sqrt((KR + FOOT_R) ** 2 - _h ** 2)
FOOT_Y = HY - _dy                       # where the foot meets the floor
_fc = (FOOT_Y, T_LOW + FOOT_R)          # centre of the concave blend
_ang = math.atan2(_h, _dy)


def _knuckle_pts():
    pts = []
    a0 = -math.pi / 2
    for i in (1, 2, 3):                  # concave blend
        a = a0 + (_ang - a0) * i / 3
        pts.append((_fc[0] + FOOT_R * math.cos(a),
                    _fc[1] + FOOT_R * math.sin(a)))
    p_start = _ang + math.pi             # on the knuckle circle
    p_end = math.asin((T_MAIN - 0.3 - HZ) / KR)
    n = 9
    for i in range(1, n + 1):            # round top down to the slab
        a = p_start + (p_end - p_start) * i / n
        pts.append((HY + KR * math.cos(a), HZ + KR * math.sin(a)))
    t_end = (math.sin(p_end), -math.cos(p_end))
    return pts, t_end


_KPTS, _KTEND = _knuckle_pts()


def k_prof():
    ye = _KPTS[-1][0]
    allp = [(FOOT_Y, T_LOW)] + _KPTS
    par = [0.0]                          # chord-length parametrisation
    for a, b in zip(allp[:-1], allp[1:]):
        par.append(par[-1] + math.dist(a, b))
    return (cq.Workplane("YZ")
            .moveTo(FOOT_Y, T_LOW - 0.2)
            .lineTo(FOOT_Y, T_LOW)
            .spline(_KPTS, tangents=[(1, 0), _KTEND], parameters=par,
                    scale=False, includeCurrent=True)
            .lineTo(ye, T_LOW - 0.2)
            .close())


knuck_x = []
for k in range(N_K):
    x0 = K_START + (k - 1) * K_PITCH
    x1 = x0 + K_W
    x0c, x1c = max(x0, 0.0), min(x1, W)
    knuck_x.append((x0c, x1c))
    kn = k_prof().extrude(x1c - x0c).translate((x0c, 0, 0))
    plate = plate.union(kn)

# clearance notches between the knuckles
def notch(gx0, gx1):
    """gap between knuckles: cut down to the low floor, back wall with a
    rounded top edge"""
    c = (NOTCH_Y + NOTCH_R, T_MAIN - NOTCH_R)
    mid = (c[0] - NOTCH_R * math.cos(math.pi / 4),
           c[1] + NOTCH_R * math.sin(math.pi / 4))
    return (cq.Workplane("YZ")
            .moveTo(FOOT_Y - 1.0, NOTCH_Z)
            .lineTo(NOTCH_Y, NOTCH_Z)
            .lineTo(NOTCH_Y, c[1])
            .threePointArc(mid, (c[0], T_MAIN))
            .lineTo(c[0], T_MAIN + 10)
            .lineTo(FOOT_Y - 1.0, T_MAIN + 10)
            .close()
            .extrude(gx1 - gx0)
            .translate((gx0, 0, 0)))


for i in range(len(knuck_x) - 1):
    plate = plate.cut(notch(knuck_x[i][1], knuck_x[i + 1][0]))

# pin hole through all knuckles
pin = (cq.Workplane("YZ").center(HY, HZ).circle(PIN_R).extrude(W + 10)
       .translate((-5, 0, 0)))
plate = plate.cut(pin)

# ---------------------------------------------------------------
# bosses at the hinge end
# ---------------------------------------------------------------
def corner_boss(c1, r1, c2, r2):
    """teardrop boss at a plate corner: convex hull of the plate corner
    rounding circle (c1, r1) and the boss circle (c2, r2)"""
    dx, dy = c2[0] - c1[0], c2[1] - c1[1]
    dd = math.hypot(dx, dy)
    th = math.atan2(dy, dx)
    ph = math.acos((r1 - r2) / dd)
    n_p = (math.cos(th + ph), math.sin(th + ph))
    n_m = (math.cos(th - ph), math.sin(th - ph))
    t1p = (c1[0] + r1 * n_p[0], c1[1] + r1 * n_p[1])
    t2p = (c2[0] + r2 * n_p[0], c2[1] + r2 * n_p[1])
    t1m = (c1[0] + r1 * n_m[0], c1[1] + r1 * n_m[1])
    t2m = (c2[0] + r2 * n_m[0], c2[1] + r2 * n_m[1])
    far = (c2[0] + r2 * math.cos(th), c2[1] + r2 * math.sin(th))
    near = (c1[0] - r1 * math.cos(th), c1[1] - r1 * math.sin(th))
    return (cq.Workplane("XY")
            .moveTo(*t1p).lineTo(*t2p)
            .threePointArc(far, t2m)
            .lineTo(*t1m)
            .threePointArc(near, t1p)
            .close()
            .extrude(BOSS_TOP))


bosses = corner_boss((CORNER_R, CORNER_R), CORNER_R,
                     (HOLE_X, HOLE_Y1), CBOSS_R)
bosses = bosses.union(corner_boss((W - CORNER_R, CORNER_R), CORNER_R,
                                  (W - HOLE_X, HOLE_Y1), CBOSS_R))
for x in (HOLE_X, W - HOLE_X):
    bosses = bosses.union(cq.Workplane("XY").center(x, HOLE_Y2)
                          .circle(BOSS_R).extrude(BOSS_TOP))
plate = plate.union(bosses)

holes = (cq.Workplane("XY")
         .pushPoints([(HOLE_X, HOLE_Y1), (W - HOLE_X, HOLE_Y1),
                      (HOLE_X, HOLE_Y2), (W - HOLE_X, HOLE_Y2)])
         .circle(HOLE_R).extrude(40).translate((0, 0, -5)))
plate = plate.cut(holes)

# centre counterbored hole
plate = plate.cut(cq.Workplane("XY").center(CH_X, CH_Y).circle(CH_R)
                  .extrude(40).translate((0, 0, -5)))
plate = plate.cut(cq.Workplane("XY").center(CH_X, CH_Y).circle(CB_R)
                  .extrude(CB_D + 5).translate((0, 0, T_MAIN - CB_D)))

# blind holes from the underside
bpts = [(CH_X + sx * BH_OFF, CH_Y + sy * BH_OFF)
        for sx in (-1, 1) for sy in (-1, 1)]
plate = plate.cut(cq.Workplane("XY").pushPoints(bpts).circle(BH_R)
                  .extrude(BH_D + 1).translate((0, 0, -1)))

# ---------------------------------------------------------------
# bracket at +Y end: thin base, two shaft saddles, side tab
# ---------------------------------------------------------------
sx0 = W / 2 - S_OFF - S_W / 2
sx1 = W / 2 - S_OFF + S_W / 2
tx0 = W / 2 + S_OFF - S_W / 2
tx1 = W / 2 + S_OFF + S_W / 2

# +X diagonal edge from saddle corner down to the tab
diag_end_x = tx1 + DIAG_SLOPE * (S_Y1 - TAB_Y1)
base_pts = [
    (0.0, L - 6.0),
    (0.0, L - CORNER_C),
    (sx0, S_Y1 - S_FR),
    (sx1, S_Y1 - S_FR),
    (sx1, BAR_Y),
    (tx0, BAR_Y),
    (tx0, S_Y1 - S_FR),
    (tx1, S_Y1 - S_FR),
    (diag_end_x, TAB_Y1),
    (TAB_X1 - TAB_BLK_L + 1.0, TAB_Y1),
    (TAB_X1 - TAB_BLK_L + 1.0, TAB_Y0),
    (W, TAB_Y0),
    (W, L - 6.0),
]
base = cq.Workplane("XY").polyline(base_pts).close().extrude(T_BASE)
# concave fillets where the diagonal meets the tab and tab meets plate
base = (base.edges("|Z")
        .edges(cq.selectors.NearestToPointSelector((diag_end_x, TAB_Y1, 4)))
        .fillet(TAB_FIL))
base = (base.edges("|Z")
        .edges(cq.selectors.NearestToPointSelector((W, TAB_Y0, 4)))
        .fillet(TAB_FIL2))


def saddle_block(x0, x1):
    return box(x0, x1, S_Y0, S_Y1, 0, S_TOP).edges("|Z").fillet(S_FR)


def saddle_cut(x0, x1, lip_side):
    """shaft seat (large radius) plus narrower lip on the outer side,
    and the two blind screw holes"""
    if lip_side > 0:
        seat_x0, seat_x1 = x0 - 1, x1 - LIP_W
    else:
        seat_x0, seat_x1 = x0 + LIP_W, x1 + 1
    seat = (cq.Workplane("YZ").center(U_Y, U_Z).circle(U_R)
            .extrude(seat_x1 - seat_x0).translate((seat_x0, 0, 0)))
    lip = (cq.Workplane("YZ").center(U_Y, U_Z).circle(LIP_R)
           .extrude(x1 - x0 + 2).translate((x0 - 1, 0, 0)))
    xc = (x0 + x1) / 2
    hl = (cq.Workplane("XY")
          .pushPoints([(xc, y) for y in S_HOLE_Y])
          .circle(S_HOLE_R).extrude(S_HOLE_D + 1)
          .translate((0, 0, S_TOP - S_HOLE_D)))
    return seat.union(lip).union(hl)


s1 = saddle_block(sx0, sx1)
s2 = saddle_block(tx0, tx1)

tab_blk = (box(TAB_X1 - TAB_BLK_L, TAB_X1, TAB_Y0, TAB_Y1, 0, TAB_BLK_TOP)
           .edges("|Z and >X").fillet(TAB_BLK_R))

bracket = base.union(s1).union(s2).union(tab_blk)

part = plate.union(bracket)
part = part.cut(saddle_cut(sx0, sx1, -1)).cut(saddle_cut(tx0, tx1, +1))

# centre the part on the origin in XY
result = part.translate((-W / 2, -(S_Y1) / 2, 0))
